import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
TILE = 10.0          # floor tile pitch
NT = 7               # tiles per side
WALL = 5.0           # wall thickness
FLOOR_T = 5.0        # floor slab thickness
HEIGHT = 65.5        # overall height (floor bottom to wall top)
TILE_T = 2.2         # tile thickness
TILE_GAP = 0.2       # grout gap between tiles
TILE_R = 0.15        # tile top edge round

SIZE = WALL + NT * TILE          # overall footprint (square)
X0 = -SIZE / 2.0                 # outer -X face (left wall outside)
Y0 = -SIZE / 2.0                 # front edge of floor
XI = X0 + WALL                   # inner face of left wall
YI = -Y0 - WALL                  # inner face of back wall
ZF = FLOOR_T + TILE_T            # finished floor level (tile top)

# fridge
FR_X0, FR_X1, FR_XD = XI + 0.3, -14.0, -8.9
FR_Y0, FR_Y1 = 9.75, 30.4
FR_TOP = 56.6
FR_R_BODY = 4.5
FR_R_DOOR_TOP = 4.5  # door top edge rounds
FR_R_DOOR = 1.8      # door vertical front edge rounds

# lower kitchen unit
LC_X1 = -13.3         # cabinet body front
LC_DOOR_T = 1.6
LC_Y0, LC_Y1 = -36.6, 6.9
LC_TOP = 30.0
CT_T = 3.3            # counter top thickness
CT_X1 = -11.3
SINK = (-28.6, -13.9, -34.3, -19.4, 3.0)   # x0,x1,y0,y1,height

# upper cabinet
UC_X1 = -20.5
UC_Z0, UC_Z1 = 51.4, HEIGHT - 0.8
UC_DOOR_T = 1.8

# table
TB_X0, TB_X1 = 10.3, 34.8
TB_Y0, TB_Y1 = Y0, 3.0
TB_Z1 = 27.3
TB_T = 2.8
LEG = 4.3
LEG_IN = 2.2

# boiler on back wall + outdoor unit behind it
BO_X0, BO_X1 = 4.4, 27.1
BO_Z0, BO_Z1 = 31.1, 58.9
BO_DEPTH = 11.5
OU_DEPTH = 6.1


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0)
            .translate(((x0 + x1) / 2, (y0 + y1) / 2, (z0 + z1) / 2)))


# ---------------- room shell ----------------
room = box(X0, -X0, Y0, -Y0, 0, FLOOR_T)
room = room.union(box(X0, XI, Y0, -Y0, 0, HEIGHT))
room = room.union(box(X0, -X0, YI, -Y0, 0, HEIGHT))

# floor tiles
tile = box(0, TILE - TILE_GAP, 0, TILE - TILE_GAP, FLOOR_T - 0.01, ZF)
if TILE_R > 0:
    tile = tile.faces(">Z").edges().fillet(TILE_R)
tiles = None
for i in range(NT):
    for j in range(NT):
        t = tile.translate((XI + i * TILE + TILE_GAP / 2,
                            Y0 + j * TILE + TILE_GAP / 2, 0))
        tiles = t if tiles is None else tiles.union(t)
room = room.union(tiles)

# ---------------- fridge ----------------
fr_body = (box(FR_X0, FR_X1, FR_Y0, FR_Y1, ZF, FR_TOP)
           .faces(">Z").edges("not >X").fillet(FR_R_BODY))
fr_door = (box(FR_X1 - 0.3, FR_XD, FR_Y0, FR_Y1, ZF, FR_TOP)
           .faces(">Z").edges("not <X").fillet(FR_R_DOOR_TOP)
           .edges("|Z").edges(">X").fillet(FR_R_DOOR))
hy = 15.7
fr_handle = (box(FR_XD - 0.3, FR_XD + 3.4, hy - 1.5, hy + 1.5, 33.4, 35.6)
             .union(box(FR_XD + 1.4, FR_XD + 3.4, hy - 1.5, hy + 1.5, 28.3, 33.5))
             .edges().fillet(0.4))
fridge = fr_body.union(fr_door).union(fr_handle)

# ---------------- lower kitchen unit ----------------
lc = box(XI - 0.01, LC_X1, LC_Y0, LC_Y1, ZF - 0.01, LC_TOP).edges("|Z and >X").fillet(0.3)
ymid = (LC_Y0 + LC_Y1) / 2.0
for (a, b) in ((LC_Y0 + 0.6, ymid - 0.4), (ymid + 0.4, LC_Y1 - 0.6)):
    d = (box(LC_X1 - 0.01, LC_X1 + LC_DOOR_T, a, b, 10.6, LC_TOP - 0.4)
         .edges(">X").fillet(0.35))
    lc = lc.union(d)
for yk in (ymid - 2.9, ymid + 2.9):
    k = cq.Workplane("XY").sphere(1.2).translate((LC_X1 + LC_DOOR_T + 0.5, yk, 20.6))
    lc = lc.union(k)
ctop = (box(XI - 0.01, CT_X1, LC_Y0 - 0.4, LC_Y1 + 0.2, LC_TOP, LC_TOP + CT_T)
        .edges("not <X").fillet(0.5))
lc = lc.union(ctop)
sx0, sx1, sy0, sy1, sh = SINK
sink = (box(sx0, sx1, sy0, sy1, LC_TOP + CT_T - 0.01, LC_TOP + CT_T + sh)
        .edges().fillet(0.3))
lc = lc.union(sink)
# faucet: inverted L made of a rounded bar
fz0 = LC_TOP + CT_T + sh
FAU_X, FAU_Y, FAU_W, FAU_T, FAU_H, FAU_L = -27.9, -27.2, 1.7, 1.1, 3.5, 5.6
faucet = (cq.Workplane("XZ")
          .moveTo(FAU_X, fz0 - 0.5).lineTo(FAU_X, fz0 + FAU_H).lineTo(FAU_X + FAU_L, fz0 + FAU_H)
          .lineTo(FAU_X + FAU_L, fz0 + FAU_H - FAU_T).lineTo(FAU_X + FAU_T, fz0 + FAU_H - FAU_T)
          .lineTo(FAU_X + FAU_T, fz0 - 0.5)
          .close().extrude(FAU_W / 2.0, both=True)
          .translate((0, FAU_Y, 0))
          .edges("|Y").fillet(0.3)
          .faces("not <Z").edges("not |Y").fillet(0.2))
lc = lc.union(faucet)

# ---------------- upper cabinet ----------------
uc = box(XI - 0.01, UC_X1, LC_Y0, LC_Y1, UC_Z0, UC_Z1).edges("not <X").fillet(0.4)
for (a, b) in ((LC_Y0 + 0.6, ymid - 0.4), (ymid + 0.4, LC_Y1 - 0.6)):
    d = (box(UC_X1 - 0.01, UC_X1 + UC_DOOR_T, a, b, UC_Z0 + 0.4, UC_Z1 - 0.4)
         .edges(">X").fillet(0.4))
    uc = uc.union(d)
for yk in (ymid - 2.9, ymid + 2.9):
    k = cq.Workplane("XY").sphere(1.4).translate((UC_X1 + UC_DOOR_T + 0.7, yk, 58.0))
    uc = uc.union(k)

# ---------------- table ----------------
table = (box(TB_X0, TB_X1, TB_Y0, TB_Y1, TB_Z1 - TB_T, TB_Z1)
         .edges().fillet(0.4))
for lx in (TB_X0 + LEG_IN, TB_X1 - LEG_IN - LEG):
    for ly in (TB_Y0 + LEG_IN, TB_Y1 - LEG_IN - LEG):
        table = table.union(box(lx, lx + LEG, ly, ly + LEG, ZF - 0.01, TB_Z1 - TB_T + 0.01))


def cup(x, y):
    prof = (cq.Workplane("XZ")
            .moveTo(0, 0).lineTo(1.9, 0).lineTo(2.75, 5.7)
            .threePointArc((2.42, 6.0), (2.05, 5.7))
            .lineTo(1.35, 0.9).lineTo(0, 0.9).close()
            .revolve(360, (0, 0, 0), (0, 1, 0)))
    return prof.translate((x, y, TB_Z1 - 0.01))


def plate(x, y):
    prof = (cq.Workplane("XZ")
            .moveTo(0, 0).lineTo(4.0, 0).lineTo(6.3, 1.0).lineTo(6.3, 1.3)
            .lineTo(5.8, 1.3).lineTo(4.2, 0.5).lineTo(0, 0.5).close()
            .revolve(360, (0, 0, 0), (0, 1, 0)))
    return prof.translate((x, y, TB_Z1 - 0.01))


table = table.union(cup(16.7, -14.8)).union(cup(25.2, -27.35)).union(plate(25.3, -6.8))

# ---------------- boiler + outdoor unit ----------------
boiler = box(BO_X0, BO_X1, YI - BO_DEPTH, YI + 0.01, BO_Z0, BO_Z1)
boiler = boiler.union(box(BO_X0 + 0.3, BO_X1 - 0.3, YI - 4.5, YI + 0.01, BO_Z0 - 3.0, BO_Z0 + 0.01))
outdoor = box(BO_X0, BO_X1, -Y0 - 0.01, -Y0 + OU_DEPTH, BO_Z0, BO_Z1)

result = (room.union(fridge).union(lc).union(uc).union(table)
          .union(boiler).union(outdoor))

VIEW = {"azimuth": 45, "elevation": 26}
